import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
R = 20.0            # outer radius of the clamp ring
H = 43.4            # height of the clamp ring
R_BORE = 15.75      # bore radius
RIM_FILLET = 2.2    # fillet on the outer top / bottom ring edges

SPLIT_W = 3.8       # width of the clamping split

# clamp lug (back side, +Y), tapered in plan and in elevation
LUG_LEN = 39.0      # tip distance from ring axis
LUG_HW0 = 20.5      # half width of the lug planes at the axis (plan)
LUG_HW1 = 4.1       # half width at the tip (plan)
LUG_HH0 = 20.8      # half height at the axis (elevation)
LUG_HH1 = 10.5      # half height at the tip (elevation)
LUG_TIP_R = 2.0     # rounding of the tip corners (plan)
LUG_Y0 = 6.0        # lug prism starts inside the ring wall

SCREW_Y = 27.5      # screw axis distance from ring axis
SCREW_R = 2.3       # screw clearance hole radius
CBORE_R = 9.9       # spot face radius, +X flank (screw head side)
CBORE_X = 4.5       # spot face floor distance from mid plane, +X flank
CBORE2_R = 7.4      # spot face radius, -X flank (nut side)
CBORE2_X = 4.5      # spot face floor distance from mid plane, -X flank

# arm (front side, -Y), offset to +X, flush with the ring tangent
ARM_X0 = 6.9
ARM_X1 = R
ARM_LEN = 50.0      # arm end distance from ring axis
ARM_Z0 = -12.9
ARM_Z1 = 17.3
ARM_END_R = 2.5     # rounding of the arm end vertical edges
ARM_ROOT_R = 2.7    # fillet where the arm meets the ring

PIN_R = 4.3         # keyhole pin bore radius at the arm end
PIN_DEPTH = 25.9    # depth of the pin bore from the arm top
PIN_SLOT_W = 4.2    # slot from the pin bore to the end face

# ---------------- ring ----------------
ring = (
    cq.Workplane("XY")
    .workplane(offset=-H / 2)
    .circle(R)
    .extrude(H)
    .edges("%CIRCLE")
    .fillet(RIM_FILLET)
)

# ---------------- arm ----------------
arm_w = ARM_X1 - ARM_X0
arm_h = ARM_Z1 - ARM_Z0
arm = (
    cq.Workplane("XY")
    .box(arm_w, ARM_LEN, arm_h, centered=False)
    .translate((ARM_X0, -ARM_LEN, ARM_Z0))
    .edges("|Z")
    .edges(cq.selectors.BoxSelector((ARM_X0 - 1, -ARM_LEN - 1, ARM_Z0 - 1),
                                    (ARM_X1 + 1, -ARM_LEN + 1, ARM_Z1 + 1)))
    .fillet(ARM_END_R)
)

# ---------------- lug ----------------
hw0 = LUG_HW0 - (LUG_HW0 - LUG_HW1) * LUG_Y0 / LUG_LEN
hh0 = LUG_HH0 - (LUG_HH0 - LUG_HH1) * LUG_Y0 / LUG_LEN
plan = (
    cq.Workplane("XY")
    .workplane(offset=-H / 2)
    .polyline([(-hw0, LUG_Y0), (hw0, LUG_Y0), (LUG_HW1, LUG_LEN), (-LUG_HW1, LUG_LEN)])
    .close()
    .extrude(H)
    .edges("|Z")
    .edges(cq.selectors.BoxSelector((-50, LUG_LEN - 0.5, -50), (50, LUG_LEN + 0.5, 50)))
    .fillet(LUG_TIP_R)
)
elev = (
    cq.Workplane("YZ")
    .workplane(offset=-2 * R)
    .polyline([(LUG_Y0, -hh0), (LUG_LEN, -LUG_HH1), (LUG_LEN, LUG_HH1), (LUG_Y0, hh0)])
    .close()
    .extrude(4 * R)
)
lug = plan.intersect(elev)

# ---------------- combine ----------------
body = ring.union(arm).union(lug)

# fillet at the root of the arm (-X side, concave vertical edge)
root_y = -math.sqrt(R * R - ARM_X0 * ARM_X0)
body = body.edges(
    cq.selectors.BoxSelector((ARM_X0 - 0.3, root_y - 0.3, ARM_Z0 - 1),
                             (ARM_X0 + 0.3, root_y + 0.3, ARM_Z1 + 1))
).fillet(ARM_ROOT_R)

# bore
bore = cq.Workplane("XY").workplane(offset=-H).circle(R_BORE).extrude(2 * H)
body = body.cut(bore)

# clamping split through the back wall and the lug
split = cq.Workplane("XY").box(SPLIT_W, LUG_LEN + 5, 2 * H, centered=(True, False, True))
body = body.cut(split)

# screw hole along X through the lug
screw = (
    cq.Workplane("YZ")
    .workplane(offset=-2 * R)
    .center(SCREW_Y, 0)
    .circle(SCREW_R)
    .extrude(4 * R)
)
body = body.cut(screw)

# flat-bottomed spot faces on both lug flanks (floors normal to the screw axis)
for x_start, cb_r, cb_len in (
    (CBORE_X, CBORE_R, 2 * R - CBORE_X),        # +X flank, from the floor outward
    (-2 * R, CBORE2_R, 2 * R - CBORE2_X),       # -X flank, from outside in to the floor
):
    cb = (
        cq.Workplane("YZ")
        .workplane(offset=x_start)
        .center(SCREW_Y, 0)
        .circle(cb_r)
        .extrude(cb_len)
    )
    body = body.cut(cb)

# keyhole at the arm end: blind pin bore plus slot to the end face
pin_x = 0.5 * (ARM_X0 + ARM_X1)
pin_y = -ARM_LEN + PIN_R
pin_z0 = ARM_Z1 - PIN_DEPTH
pin = (
    cq.Workplane("XY")
    .workplane(offset=pin_z0)
    .center(pin_x, pin_y)
    .circle(PIN_R)
    .extrude(PIN_DEPTH + 5)
)
body = body.cut(pin)
pslot = (
    cq.Workplane("XY")
    .box(PIN_SLOT_W, PIN_R + 2, PIN_DEPTH + 5, centered=(True, False, False))
    .translate((pin_x, -ARM_LEN - 2, pin_z0))
)
body = body.cut(pslot)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
